import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_W = 100.0          # square base plate side
PLATE_T = 4.8            # base plate thickness
PLATE_CORNER_R = 27.0    # plan-view corner radius
EDGE_FILLET = 2.8        # rounded top outer edge

GROOVE_R_IN = 35.7       # annular groove inner radius
GROOVE_R_OUT = 38.9      # annular groove outer radius
GROOVE_DEPTH = 2.2
NOTCH_R_OUT = 40.3       # key notches at +/-X extend to this radius
NOTCH_W = 7.8            # notch width (along Y)

BIG_HOLE_D = 15.6        # 4 big holes on the diagonals
BIG_HOLE_R = 23.8        # pitch radius of the big holes
SMALL_HOLE_D = 9.4       # 4 small holes on the X / Y axes
SMALL_HOLE_R = 23.9      # pitch radius of the small holes

CORNER_HOLE_POS = 33.3   # countersunk mounting holes at (+-pos, +-pos)
CORNER_HOLE_D = 4.6
CORNER_CSK_D = 10.0
CORNER_CSK_ANGLE = 90.0

COL_BASE_R = 11.4        # flared column radius at the plate
COL_WAIST_R = 7.72       # smallest column radius (arc becomes vertical)
COL_WAIST_Z = 18.0       # height of the waist above the plate
COL_H = 20.0             # column height above the plate

HEX_AF = 13.4            # hex across flats (corners point along +-X)
HEX_H = 9.2              # hex height

PIN_HOLE_D = 2.6         # blind stepped hole in the hex top
PIN_HOLE_DEPTH = 10.0
PIN_CBORE_D = 3.7
PIN_CBORE_DEPTH = 2.0

# angular position of the seams of revolved / cylindrical faces (cosmetic:
# keeps seam edges away from the faces seen in the default view)
SEAM_COL = 100.0
SEAM_GROOVE = 45.0
SEAM_HOLE = 45.0

z_top = PLATE_T
Z_AXIS = ((0, 0, 0), (0, 0, 1))


def revolve_xz(points, seam_deg=0.0):
    """Revolve a closed (r, z) polyline about the Z axis, seam at seam_deg."""
    wp = cq.Workplane("XZ").polyline(points).close()
    solid = wp.revolve(360, (0, 0, 0), (0, 1, 0)).val()
    return solid.rotate(Z_AXIS[0], Z_AXIS[1], seam_deg)


def cylinder(r, z0, h, x=0.0, y=0.0, seam_deg=0.0):
    solid = cq.Solid.makeCylinder(r, h, cq.Vector(0, 0, z0))
    return solid.rotate(Z_AXIS[0], Z_AXIS[1], seam_deg).translate(cq.Vector(x, y, 0))


# ---------------- base plate: rounded square with rounded top edge ----------------
plate = (
    cq.Workplane("XY")
    .sketch()
    .rect(PLATE_W, PLATE_W)
    .vertices()
    .fillet(PLATE_CORNER_R)
    .finalize()
    .extrude(PLATE_T)
)
plate = plate.faces(">Z").edges().fillet(EDGE_FILLET)

# ---------------- annular groove with two key notches on +-X ----------------
z_groove = z_top - GROOVE_DEPTH
groove = revolve_xz(
    [(GROOVE_R_IN, z_groove), (GROOVE_R_OUT, z_groove),
     (GROOVE_R_OUT, z_top + 1.0), (GROOVE_R_IN, z_top + 1.0)],
    SEAM_GROOVE,
)
notch_r0 = GROOVE_R_IN + 0.5
notch_len = NOTCH_R_OUT - notch_r0
notch_cx = 0.5 * (NOTCH_R_OUT + notch_r0)
notches = (
    cq.Workplane("XY")
    .workplane(offset=z_groove)
    .pushPoints([(notch_cx, 0), (-notch_cx, 0)])
    .rect(notch_len, NOTCH_W)
    .extrude(GROOVE_DEPTH + 1.0)
)
plate = plate.cut(cq.Workplane("XY").add(groove)).cut(notches)

# ---------------- through holes: 4 big on diagonals, 4 small on axes ----------------
holes = []
for k in range(4):
    a = math.radians(45.0 + 90.0 * k)
    holes.append(cylinder(BIG_HOLE_D / 2.0, -1.0, PLATE_T + 2.0,
                          BIG_HOLE_R * math.cos(a), BIG_HOLE_R * math.sin(a), SEAM_HOLE))
    b = math.radians(90.0 * k)
    holes.append(cylinder(SMALL_HOLE_D / 2.0, -1.0, PLATE_T + 2.0,
                          SMALL_HOLE_R * math.cos(b), SMALL_HOLE_R * math.sin(b), SEAM_HOLE))

# countersunk corner holes (revolved cutter: through bore + 90 deg cone)
t_half = math.tan(math.radians(CORNER_CSK_ANGLE / 2.0))
csk_h = (CORNER_CSK_D - CORNER_HOLE_D) / 2.0 / t_half    # cone depth below the top face
csk_over = 1.0                                             # cone continues 1 mm above
csk_cutter = revolve_xz(
    [(0, -1.0), (CORNER_HOLE_D / 2.0, -1.0), (CORNER_HOLE_D / 2.0, z_top - csk_h),
     (CORNER_CSK_D / 2.0 + csk_over * t_half, z_top + csk_over), (0, z_top + csk_over)],
    SEAM_HOLE,
)
c = CORNER_HOLE_POS
for sx, sy in [(1, 1), (-1, 1), (-1, -1), (1, -1)]:
    holes.append(csk_cutter.translate(cq.Vector(sx * c, sy * c, 0)))

plate = plate.cut(cq.Workplane("XY").add(holes))

# ---------------- flared column: one concave arc, vertical at the waist ----------------
dr = COL_BASE_R - COL_WAIST_R
rc = (dr ** 2 + COL_WAIST_Z ** 2) / (2.0 * dr)       # concave arc radius
cx, cz = COL_WAIST_R + rc, z_top + COL_WAIST_Z        # arc centre (r, z)


def arc_r(z):
    return cx - math.sqrt(rc ** 2 - (z - cz) ** 2)


z_col_top = z_top + COL_H
z_mid = z_top + 0.5 * COL_H
col_wp = (
    cq.Workplane("XZ")
    .moveTo(0, z_top - 1.0)
    .lineTo(COL_BASE_R, z_top - 1.0)
    .lineTo(COL_BASE_R, z_top)
    .threePointArc((arc_r(z_mid), z_mid), (arc_r(z_col_top), z_col_top))
    .lineTo(0, z_col_top)
    .close()
)
column = col_wp.revolve(360, (0, 0, 0), (0, 1, 0)).val().rotate(Z_AXIS[0], Z_AXIS[1], SEAM_COL)

# ---------------- hex head (corners on +-X) ----------------
z_hex = z_col_top
hex_ac = HEX_AF / math.cos(math.radians(30))
hex_head = (
    cq.Workplane("XY").workplane(offset=z_hex - 0.5)
    .polygon(6, hex_ac)
    .extrude(HEX_H + 0.5)
)

result = plate.union(cq.Workplane("XY").add(column)).union(hex_head)

# blind stepped pin hole in the hex top
z_hex_top = z_hex + HEX_H
pin_cutter = revolve_xz(
    [(0, z_hex_top - PIN_HOLE_DEPTH), (PIN_HOLE_D / 2.0, z_hex_top - PIN_HOLE_DEPTH),
     (PIN_HOLE_D / 2.0, z_hex_top - PIN_CBORE_DEPTH), (PIN_CBORE_D / 2.0, z_hex_top - PIN_CBORE_DEPTH),
     (PIN_CBORE_D / 2.0, z_hex_top + 1.0), (0, z_hex_top + 1.0)],
    SEAM_HOLE,
)
result = result.cut(cq.Workplane("XY").add(pin_cutter))

VIEW = {"azimuth": 45, "elevation": 26}
